import cadquery as cq
import math

# ---------------- driving dimensions (mm) ----------------
base_d = 200.0        # outer diameter at the bottom rim
top_d = 140.5         # outer diameter of the flat top
height = 48.5         # overall height
wall = 3.0            # shell wall thickness (cone wall and top plate)
rim_fillet = 1.5      # rounding on the outer bottom edge
hole_pcd_r = 56.2     # radius of bolt circle for the three holes
hole_d = 17.5         # through hole diameter
boss_od = 22.5        # boss outer diameter (underside)
boss_drop = 16.0      # boss length below the underside of the top plate
boss_chamfer = 1.0    # chamfer on the hole mouth at the boss end
center_hole_d = 8.2   # small centre hole
hole_angles = [-90.0, 30.0, 150.0]
body_seam = 90.0     # periodic-face seam turned to the back, out of the main view
hole_seam = 45.0

rb = base_d / 2.0
rt = top_d / 2.0

# ---------------- body: hollow truncated cone (revolved profile) ----------------
slope = math.atan2(rb - rt, height)      # cone half-angle from vertical
dx = wall / math.cos(slope)              # horizontal offset of the inner cone surface
zi = height - wall                       # underside of the top plate
ri_bot = rb - dx                         # inner radius at z = 0
ri_top = ri_bot - (rb - rt) * zi / height

profile = [
    (0.0, height),
    (rt, height),
    (rb, 0.0),
    (ri_bot, 0.0),
    (ri_top, zi),
    (0.0, zi),
]
body = (
    cq.Workplane("XZ")
    .polyline(profile)
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
    .rotate((0, 0, 0), (0, 0, 1), body_seam)
)

# round the outer bottom edge
rim_edges = [e for e in body.edges("%CIRCLE").vals()
             if abs(e.Center().z) < 1e-6 and abs(e.radius() - rb) < 1e-3]
body = body.newObject(rim_edges).fillet(rim_fillet)

# ---------------- bosses under the top plate ----------------
pts = [(hole_pcd_r * math.cos(math.radians(a)), hole_pcd_r * math.sin(math.radians(a)))
       for a in hole_angles]


def cyl(r, z0, h, x, y, seam=hole_seam):
    """Vertical cylinder at (x, y) from z0, height h, seam turned to angle `seam`."""
    c = cq.Solid.makeCylinder(r, h, cq.Vector(x, y, z0), cq.Vector(0, 0, 1))
    return cq.Workplane().add(c.rotate(cq.Vector(x, y, 0), cq.Vector(x, y, 1), seam))


boss_z0 = zi - boss_drop
for (x, y) in pts:
    body = body.union(cyl(boss_od / 2.0, boss_z0, boss_drop + wall / 2, x, y))

# ---------------- through holes with chamfered mouth at the boss end ----------------
for (x, y) in pts:
    body = body.cut(cyl(hole_d / 2.0, boss_z0 - 1, height - boss_z0 + 2, x, y))
    cham = cq.Solid.makeCone(hole_d / 2.0 + boss_chamfer + 0.5, hole_d / 2.0 - 0.01,
                             boss_chamfer + 0.5 + 0.01,
                             cq.Vector(x, y, boss_z0 - 0.5), cq.Vector(0, 0, 1))
    cham = cham.rotate(cq.Vector(x, y, 0), cq.Vector(x, y, 1), hole_seam)
    body = body.cut(cq.Workplane().add(cham))

# ---------------- centre hole ----------------
body = body.cut(cyl(center_hole_d / 2.0, zi - 1, wall + 2, 0, 0))

result = body
